"""Arcade-style control panel plate: flat plate with swept-back rounded wings,
bowed front edge with 45 deg corner chamfers, a joystick hole and a diamond of
four button holes (both with rounded-over top edges) and four fixing holes."""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
T = 4.0                 # plate thickness

FLAT_HALF = 53.2        # half length of the straight top (back) edge
FLAT_Y = 42.7           # Y of the straight top edge
TOP_ANG = 20.4          # rise angle of the slanted top edges (deg)

SIDE_PT = (134.1, -28.0)  # lower end of the slanted outer side edge (x is +)
SIDE_ANG = 23.4         # lean of the slanted side edge from vertical (deg)
VERT_BOT_Y = -60.2      # bottom of the short vertical side edge
CHAMF = 8.8             # 45 deg corner chamfer at the front corners
FRONT_MID_Y = -74.8     # lowest point of the (slightly bowed) front edge
WING_R = 22.7           # radius of the rounded wing tips

# joystick / button holes
BIG_D = 54.6            # joystick hole
BIG_POS = (-51.8, -4.15)
BTN_D = 24.0            # button holes
BTN_C = (33.8, -1.75)   # centre of the 4-button diamond
BTN_OFF = 21.9          # distance of each button from the diamond centre
HOLE_FILLET = 3.4       # round-over of the joystick/button hole top edges (flares of the
                        # diagonal button pairs just miss each other)

# fixing holes
MNT_D = 8.5
MNT_TOP = (132.0, 64.0)
MNT_BOT = (84.9, -66.5)


# ---------------- outline ----------------
def outline_points():
    ta = math.radians(TOP_ANG)
    sa = math.radians(SIDE_ANG)
    # right half, computed then mirrored
    J = (FLAT_HALF, FLAT_Y)
    dt = (math.cos(ta), math.sin(ta))          # along top edge, outward
    P = SIDE_PT
    ds = (math.sin(sa), math.cos(sa))          # along side edge, upward/outward
    # intersection J + a*dt = P + b*ds
    det = dt[0] * (-ds[1]) - dt[1] * (-ds[0])
    rx, ry = P[0] - J[0], P[1] - J[1]
    a = (rx * (-ds[1]) - ry * (-ds[0])) / det
    C = (J[0] + a * dt[0], J[1] + a * dt[1])
    # tangent arc at the sharp wing corner C
    u1 = (-dt[0], -dt[1])   # from C back along top edge
    u2 = (-ds[0], -ds[1])   # from C down along side edge
    ang = math.acos(u1[0] * u2[0] + u1[1] * u2[1])
    tl = WING_R / math.tan(ang / 2)
    T1 = (C[0] + tl * u1[0], C[1] + tl * u1[1])
    T2 = (C[0] + tl * u2[0], C[1] + tl * u2[1])
    bis = (u1[0] + u2[0], u1[1] + u2[1])
    bl = math.hypot(*bis)
    bis = (bis[0] / bl, bis[1] / bl)
    dc = WING_R / math.sin(ang / 2)
    O = (C[0] + dc * bis[0], C[1] + dc * bis[1])
    M = (O[0] - WING_R * bis[0], O[1] - WING_R * bis[1])   # arc midpoint
    V1 = P
    V2 = (P[0], VERT_BOT_Y)
    V3 = (P[0] - CHAMF, VERT_BOT_Y - CHAMF)
    return J, T1, M, T2, V1, V2, V3


J, T1, M, T2, V1, V2, V3 = outline_points()


def mx(p):
    return (-p[0], p[1])


prof = (
    cq.Workplane("XY")
    .moveTo(*mx(J))
    .lineTo(*J)
    .lineTo(*T1)
    .threePointArc(M, T2)
    .lineTo(*V1)
    .lineTo(*V2)
    .lineTo(*V3)
    .threePointArc((0.0, FRONT_MID_Y), mx(V3))
    .lineTo(*mx(V2))
    .lineTo(*mx(V1))
    .lineTo(*mx(T2))
    .threePointArc(mx(M), mx(T1))
    .close()
)
plate = prof.extrude(T)

# joystick + button holes: plain bore with a rounded (quarter-round) top edge,
# cut with a revolved tool so the round-over is exact
btn_pts = [
    (BTN_C[0], BTN_C[1] + BTN_OFF),
    (BTN_C[0], BTN_C[1] - BTN_OFF),
    (BTN_C[0] - BTN_OFF, BTN_C[1]),
    (BTN_C[0] + BTN_OFF, BTN_C[1]),
]


def rounded_hole_tool(d, f):
    r = d / 2.0
    a = math.radians(45.0)
    z0 = T - f
    return (
        cq.Workplane("XZ")
        .moveTo(0, -1.0)
        .lineTo(r, -1.0)
        .lineTo(r, z0)
        .threePointArc((r + f - f * math.cos(a), z0 + f * math.sin(a)), (r + f, T))
        .lineTo(r + f, T + 1.0)
        .lineTo(0, T + 1.0)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )


big_tool = rounded_hole_tool(BIG_D, HOLE_FILLET)
btn_tool = rounded_hole_tool(BTN_D, HOLE_FILLET)
plate = plate.cut(big_tool.translate((BIG_POS[0], BIG_POS[1], 0)))
for p in btn_pts:
    plate = plate.cut(btn_tool.translate((p[0], p[1], 0)))

# plain fixing holes
mnt_pts = [MNT_TOP, mx(MNT_TOP), MNT_BOT, mx(MNT_BOT)]
mnt_tool = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .pushPoints(mnt_pts)
    .circle(MNT_D / 2.0)
    .extrude(T + 2.0)
)
plate = plate.cut(mnt_tool)

result = plate
